import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 90.0          # overall length (X)
D = 47.4          # overall depth (Y)
H = 50.0          # overall height (Z), bottom vertex at z=0
YV = 19.2         # bottom vertex distance from the front face
A_FRONT = 60.0    # front-lower face angle from horizontal
A_BACK = 30.0     # back-lower face angle (open side) from horizontal
R_CORNER = 2.3    # vertical edge radius
T_WALL = 1.0      # wall thickness
T_TOP = 2.8       # top plate thickness
BLOCK = 6.5       # corner blocks at both ends, thickness measured from the inner walls

# display window in the top plate
WIN_W = 48.7
WIN_D = 29.3
WIN_X = 0.26
WIN_Y0 = 13.86    # window front edge, measured from the front face
WIN_STEP = 0.45   # recess ledge width around the window
WIN_STEP_DEPTH = 0.5
NOTCH_X0 = 0.5    # deeper section of the recess on the front edge (cable notch)
NOTCH_X1 = 7.4
NOTCH_DEPTH = 1.2

# rib under the top plate behind the window, lip under its front edge
RIB_Z = 45.4
LIP_Z = 42.4
LIP_T = 1.2

# hole in the top plate (back-left)
TOP_HOLE_D = 6.5
TOP_HOLE_X = -37.4
TOP_HOLE_Y = 33.9  # from front face

# small side holes (both X walls)
SIDE_HOLE_D = 2.6
SIDE_HOLE_Y = 37.7  # from front face
SIDE_HOLE_Z = 41.35

# small hole in the back wall
BACK_HOLE_D = 2.8
BACK_HOLE_X = 35.1
BACK_HOLE_Z = 46.9

# vertical mounting holes through the front-lower face
MOUNT_D = 6.5
MOUNT_X0 = -27.5   # x of the left mounting hole
MOUNT_X1 = 28.0    # x of the right mounting hole
MOUNT_Y = 7.14     # axis position from front face

# flexure button slots
SLOT_W = 0.5
SLOT_R = 1.3
SLOT_PITCH = 4.63
SLOT_Y0 = 1.8      # leg lower end (centreline) from the front face
SLOT_Y1 = 9.7      # top segment centreline from the front face
GROUP1_X0 = -22.5  # first leg x of the 5-button group
GROUP1_N = 5
GROUP2_X0 = 13.95  # first leg x of the 2-button group
GROUP2_N = 2

# ---------------- derived ----------------
YF = -D / 2.0                    # front face y
YB = D / 2.0                     # back face y
yv = YF + YV                     # vertex y
af = math.radians(A_FRONT)
ab = math.radians(A_BACK)
Z_TOP_IN = H - T_TOP
X_END = L / 2 - T_WALL - BLOCK   # |x| where the thick end blocks start
T_END = T_WALL + BLOCK           # end-block wall thickness (front slope and back)


def above_front(offset, back_cut=True):
    """Prism along X: region above the front slope plane moved inward by
    `offset` (back_cut=False: open downwards behind it); with back_cut=True
    (offset 0) it is also bounded by the back slope plane."""
    big = 400.0
    # front plane through the vertex, inward normal (sin af, cos af) in (y,z)
    ny, nz = math.sin(af), math.cos(af)
    py, pz = yv + ny * offset, nz * offset
    dy, dz = -math.cos(af), math.sin(af)          # up-front along the face
    p1 = (py + big * dy, pz + big * dz)
    if back_cut:
        # back plane through the vertex, direction up-back
        by, bz = math.cos(ab), math.sin(ab)
        p2 = (yv + big * by, big * bz)
        pts = [(yv, 0.0), p2, (p2[0], 500.0), (p1[0], 500.0), p1]
    else:
        p0 = (py - big * dy, pz - big * dz)        # extend down-back
        pts = [p0, (p0[0] + big, p0[1]), (p0[0] + big, 500.0), (p1[0], 500.0), p1]
    return (
        cq.Workplane("YZ", origin=(-big / 2, 0, 0))
        .polyline(pts)
        .close()
        .extrude(big)
    )


def box(x0, x1, y0, y1, z0, z1):
    return (
        cq.Workplane("XY", origin=((x0 + x1) / 2, (y0 + y1) / 2, z0))
        .rect(x1 - x0, y1 - y0)
        .extrude(z1 - z0)
    )


# ---------------- outer body: rounded block cut by the two slope planes ----------------
outer = (
    cq.Workplane("XY")
    .rect(L, D)
    .extrude(H)
    .edges("|Z")
    .fillet(R_CORNER)
)
outer = outer.intersect(above_front(0.0, True))

# ---------------- inner cavity, open through the back-lower face ----------------
xi = L / 2 - T_WALL
yi0 = YF + T_WALL
yi1 = YB - T_WALL
cav_mid = box(-X_END, X_END, yi0, yi1, -60, Z_TOP_IN).intersect(above_front(T_WALL, False))
cav_end = box(-xi, xi, yi0, YB - T_END, -60, Z_TOP_IN).intersect(above_front(T_END, False))
cavity = cav_mid.union(cav_end)
body = outer.cut(cavity)

# rib under the top plate, behind the window
win_y0 = YF + WIN_Y0
win_y1 = win_y0 + WIN_D
rib = box(-X_END, X_END, win_y1, yi1 + 0.01, RIB_Z, Z_TOP_IN + 0.01)
lip = box(WIN_X - WIN_W / 2, WIN_X + WIN_W / 2, win_y0 - LIP_T, win_y0, LIP_Z, Z_TOP_IN + 0.01)
body = body.union(rib).union(lip)

# ---------------- display window with a shallow recess ----------------
win = box(WIN_X - WIN_W / 2, WIN_X + WIN_W / 2, win_y0, win_y1, Z_TOP_IN - 1, H + 5)
step = box(
    WIN_X - WIN_W / 2 - WIN_STEP,
    WIN_X + WIN_W / 2 + WIN_STEP,
    win_y0 - WIN_STEP,
    win_y1 + WIN_STEP,
    H - WIN_STEP_DEPTH,
    H + 5,
)
notch = box(NOTCH_X0, NOTCH_X1, win_y0 - WIN_STEP, win_y0 + 0.01, H - NOTCH_DEPTH, H + 5)
body = body.cut(win).cut(step).cut(notch)

# ---------------- top hole ----------------
top_hole = (
    cq.Workplane("XY", origin=(TOP_HOLE_X, YF + TOP_HOLE_Y, Z_TOP_IN - 1))
    .circle(TOP_HOLE_D / 2)
    .extrude(T_TOP + 2)
)
body = body.cut(top_hole)

# ---------------- side holes ----------------
side_hole = (
    cq.Workplane("YZ", origin=(-L, YF + SIDE_HOLE_Y, SIDE_HOLE_Z))
    .circle(SIDE_HOLE_D / 2)
    .extrude(2 * L)
)
body = body.cut(side_hole)

# ---------------- back hole (through the back wall and the rib) ----------------
back_hole = (
    cq.Workplane("XZ", origin=(BACK_HOLE_X, YB + 1, BACK_HOLE_Z))   # XZ normal is -Y
    .circle(BACK_HOLE_D / 2)
    .extrude(8)
)
body = body.cut(back_hole)

# ---------------- vertical mounting holes through the front-lower face ----------------
mount = (
    cq.Workplane("XY", origin=(0, YF + MOUNT_Y, -5))
    .pushPoints([(MOUNT_X0, 0), (MOUNT_X1, 0)])
    .circle(MOUNT_D / 2)
    .extrude(36)
)
body = body.cut(mount)


# ---------------- flexure button slots ----------------
def n_slot(x0, x1):
    ya = YF + SLOT_Y0
    yb = YF + SLOT_Y1
    r = SLOT_R
    c45 = math.cos(math.pi / 4)
    e = [
        cq.Edge.makeLine(cq.Vector(x0, ya, 0), cq.Vector(x0, yb - r, 0)),
        cq.Edge.makeThreePointArc(
            cq.Vector(x0, yb - r, 0),
            cq.Vector(x0 + r - r * c45, yb - r + r * c45, 0),
            cq.Vector(x0 + r, yb, 0),
        ),
        cq.Edge.makeLine(cq.Vector(x0 + r, yb, 0), cq.Vector(x1 - r, yb, 0)),
        cq.Edge.makeThreePointArc(
            cq.Vector(x1 - r, yb, 0),
            cq.Vector(x1 - r + r * c45, yb - r + r * c45, 0),
            cq.Vector(x1, yb - r, 0),
        ),
        cq.Edge.makeLine(cq.Vector(x1, yb - r, 0), cq.Vector(x1, ya, 0)),
    ]
    w = cq.Wire.assembleEdges(e)
    ow = w.offset2D(SLOT_W / 2, "arc")[0]
    f = cq.Face.makeFromWires(ow)
    sol = cq.Solid.extrudeLinear(f, cq.Vector(0, 0, T_TOP + 2))
    return sol.translate(cq.Vector(0, 0, Z_TOP_IN - 1))


slots = None
for x0, n in ((GROUP1_X0, GROUP1_N), (GROUP2_X0, GROUP2_N)):
    for i in range(n):
        s = n_slot(x0 + i * SLOT_PITCH, x0 + (i + 1) * SLOT_PITCH)
        slots = s if slots is None else slots.fuse(s)
body = body.cut(cq.Workplane().add(slots))

result = body.clean()
VIEW = {"azimuth": 45, "elevation": 26}
